import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 60.0            # ring outer radius
T = 5.05            # ring top face height (inner field)
T_RIM = 5.2         # raised outer rim band height
T_LINK = 5.1        # link thickness

# inner bore: short cylindrical land with a taper above and below
R_LAND = 33.0       # land radius (smallest)
Z_LAND = (1.8, 2.8) # land z-range
R_TOP = 36.6        # bore radius at top face
R_BOT = 35.3        # bore radius at bottom face

TOOTH_A = 52.0      # half width of the "cross" that forms the rim teeth
TOOTH_B = 35.6      # notch wall offset (notch between teeth at the diagonals)

BAND_W = 3.2        # outer raised band width

# snap-latch profile on the rim between the teeth of each diagonal notch
N_LIP_R = 0.9       # latch lip protrusion beyond R
N_LIP_Z = (2.2, 3.5)  # latch lip face z-range
N_SLOPE_IN = 1.7    # lead-in slope starts this far inside R at the top
N_GROOVE_Z = (1.6, 2.2)
N_GROOVE_D = 1.6    # groove depth below R
N_LOW_D = 0.7       # lower face recess below R

# +Y pocket (opens into the bore)
PK_W = 37.0
PK_YMAX = 48.3
PK_D = 3.6

# -Y slot pocket
SP_X0, SP_X1 = -24.1, 26.1
SP_Y0, SP_Y1 = -47.1, -39.0
SP_D = 2.1

# small blind holes
SH_X, SH_Y = 22.9, 34.3
SH_D = 5.0
SH_DEPTH = 4.0

# bosses
BOSS_X = 44.8
BOSS_Y = (8.0, -13.0)
BOSS_RB = 7.1       # plain (+X) cone base radius
BOSS_RT = 4.4       # plain (+X) cone top radius
BOSS_H = 11.25
BOSS_FB = 0.6       # base fillet (plain bosses)
BOSS_FT = 0.4       # top fillet
SBOSS_RB = 7.4      # slotted (-X) boss: cone base radius
SBOSS_RC = 4.7      # slotted boss: upper cylinder radius
SBOSS_HC = 3.1      # slotted boss: upper cylinder height
BOSS_HOLE_P = 3.9   # plain bosses (+X)
BOSS_HOLE_C = 5.2   # slotted bosses (-X)
BOSS_HOLE_DEPTH = 10.0
FLAT_OFF = 3.0      # flat cut distance from boss axis
FLAT_Z = 2.5        # flat cut ledge height above ring top
SLOT_W = 3.2
SLOT_DEPTH = 3.0

SEAM_ANGLE = 135.0  # angular position of revolve seams on the bosses

# links
L1_Y = 98.7
L1_X = 23.0
L1_PAD_R = 5.2
L1_FLAT = 4.2      # pad flat below hole centre
L1_BLEND = 2.0     # bar/pad concave blend
L1_BAR_END = 4.8   # bar width next to the pads
L1_BAR_MID = 3.5   # bar width at mid span (concave upper edge)
L_HOLE_D = 6.3
LINK_FILLET = 0.5

L2_X0, L2_X1 = -28.6, -2.3
L2_Y0, L2_Y1 = 66.4, 87.2
L2_LOW = 3.1
L2_HOLE_Y = 72.2
L2_END_X = 22.6
L2_END_R = 7.3
L2_ARM_TOP = 79.6
L2_ARM_BOT = 70.5          # arm lower edge where it leaves the frame
L2_ARM_MID = (8.0, 69.6)   # point on the curved lower arm edge
L2_ARM_TAN = (18.9, 66.2)  # lower arm edge meets the round end here
L2_SQ = 10.7               # square boss size (x)
L2_SQ_Y = 11.2             # square boss size (y)
L2_SQ_HOLE_X = -23.25
L2_SLOT_C = (-15.7, 77.1)  # stadium opening centre
L2_SLOT_R = 8.5            # stadium opening end radius
L2_SLOT_L = 6.4            # stadium opening straight length


def ring_body():
    # outline: circle + cross (forms teeth beside each diagonal notch)
    disc = cq.Workplane("XY").circle(R).extrude(T_RIM)
    cross = (cq.Workplane("XY").rect(2 * TOOTH_A, 2 * TOOTH_B).extrude(T_RIM)
             .union(cq.Workplane("XY").rect(2 * TOOTH_B, 2 * TOOTH_A).extrude(T_RIM)))
    body = disc.union(cross)

    # inner field sits slightly below the raised outer rim band
    field = (cq.Workplane("XY").circle(R - BAND_W).extrude(1.0).translate((0, 0, T)))
    body = body.cut(field)

    # inner bore (revolved profile cutter: lower taper, land, upper taper)
    bore = (cq.Workplane("XZ")
            .polyline([(0, -1), (R_BOT + (R_BOT - R_LAND) / Z_LAND[0], -1),
                       (R_LAND, Z_LAND[0]), (R_LAND, Z_LAND[1]),
                       (R_TOP + (R_TOP - R_LAND) / (T - Z_LAND[1]), T + 1), (0, T + 1)])
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 0, 1), -45))
    body = body.cut(bore)

    # notch regions (between the teeth at the four diagonals)
    region = None
    for sx in (1, -1):
        for sy in (1, -1):
            L = R + 10 - TOOTH_B
            bx = (cq.Workplane("XY").box(L, L, T_RIM + 4, centered=False)
                  .translate((TOOTH_B if sx > 0 else -R - 10,
                              TOOTH_B if sy > 0 else -R - 10, -2)))
            region = bx if region is None else region.union(bx)

    def rev(pts):
        return (cq.Workplane("XZ").polyline(pts).close()
                .revolve(360, (0, 0, 0), (0, 1, 0)))

    # latch lip standing proud of the rim
    lip = rev([(R - 0.5, N_LIP_Z[0]), (R + N_LIP_R, N_LIP_Z[0]),
               (R + N_LIP_R, N_LIP_Z[1]), (R - 0.5, N_LIP_Z[1])])
    body = body.union(lip.intersect(region))
    # lead-in slope, groove under the lip and recessed lower face
    cutter = (rev([(R - N_SLOPE_IN, T_RIM + 1), (R - N_SLOPE_IN, T_RIM),
                   (R + N_LIP_R, N_LIP_Z[1]), (R + 6, N_LIP_Z[1]), (R + 6, T_RIM + 1)])
              .union(rev([(R - N_GROOVE_D, N_GROOVE_Z[0]), (R + 6, N_GROOVE_Z[0]),
                          (R + 6, N_GROOVE_Z[1]), (R - N_GROOVE_D, N_GROOVE_Z[1])]))
              .union(rev([(R - N_LOW_D, -1), (R + 6, -1), (R + 6, N_GROOVE_Z[0]),
                          (R - N_LOW_D, N_GROOVE_Z[0])])))
    body = body.cut(cutter.intersect(region))

    # +Y pocket opening into the bore
    pk = (cq.Workplane("XY").box(PK_W, PK_YMAX, PK_D + 1, centered=False)
          .translate((-PK_W / 2, 0, T - PK_D)))
    body = body.cut(pk)

    # -Y slot pocket
    sp = (cq.Workplane("XY").box(SP_X1 - SP_X0, SP_Y1 - SP_Y0, SP_D + 1, centered=False)
          .translate((SP_X0, SP_Y0, T - SP_D)))
    body = body.cut(sp)

    # small blind holes
    holes = (cq.Workplane("XY").pushPoints([(sx * SH_X, sy * SH_Y) for sx in (1, -1) for sy in (1, -1)])
             .circle(SH_D / 2).extrude(SH_DEPTH + 1).translate((0, 0, T - SH_DEPTH)))
    body = body.cut(holes)
    return body


def _fillet_pts(p_prev, corner, p_next, rad):
    """Tangent points and mid point of a fillet of radius rad at a polyline corner."""
    ux, uy = p_prev[0] - corner[0], p_prev[1] - corner[1]
    lu = math.hypot(ux, uy)
    ux, uy = ux / lu, uy / lu
    vx, vy = p_next[0] - corner[0], p_next[1] - corner[1]
    lv = math.hypot(vx, vy)
    vx, vy = vx / lv, vy / lv
    ang = math.acos(max(-1.0, min(1.0, ux * vx + uy * vy)))
    t = rad / math.tan(ang / 2)
    a = (corner[0] + ux * t, corner[1] + uy * t)
    b = (corner[0] + vx * t, corner[1] + vy * t)
    bx, by = ux + vx, uy + vy
    lb = math.hypot(bx, by)
    dc = rad / math.sin(ang / 2)
    c = (corner[0] + bx / lb * dc, corner[1] + by / lb * dc)
    m = (c[0] - bx / lb * rad, c[1] - by / lb * rad)
    return a, m, b


def revolved_boss(x, y, z0, pts, radii):
    """Revolve a boss outline (r, z) polyline with filleted corners about a vertical axis.
    pts runs from the base (r_base_flange, 0) to the top (0, h); radii gives the
    fillet radius at each interior corner (0 = sharp)."""
    wp = cq.Workplane("XZ").moveTo(0, -0.6).lineTo(pts[0][0], -0.6).lineTo(*pts[0])
    for i in range(1, len(pts) - 1):
        rad = radii[i - 1]
        if rad > 0:
            a, m, b = _fillet_pts(pts[i - 1], pts[i], pts[i + 1], rad)
            wp = wp.lineTo(*a).threePointArc(m, b)
        else:
            wp = wp.lineTo(*pts[i])
    wp = wp.lineTo(*pts[-1]).close()
    # seam placed on the side facing away from the default camera
    return (wp.revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).translate((x, y, z0)))


def boss(x, y, slotted, flat_dir):
    top = T + BOSS_H
    if slotted:
        pts = [(SBOSS_RB + 0.9, 0), (SBOSS_RB, 0), (SBOSS_RC, BOSS_H - SBOSS_HC),
               (SBOSS_RC, BOSS_H), (0, BOSS_H)]
        b = revolved_boss(x, y, T, pts, [0.0, 1.5, BOSS_FT])
    else:
        pts = [(BOSS_RB + 0.9, 0), (BOSS_RB, 0), (BOSS_RT, BOSS_H), (0, BOSS_H)]
        b = revolved_boss(x, y, T, pts, [BOSS_FB, BOSS_FT])
    hole_d = BOSS_HOLE_C if slotted else BOSS_HOLE_P
    b = b.cut(cq.Workplane("XY").circle(hole_d / 2).extrude(BOSS_HOLE_DEPTH + 1)
              .translate((x, y, top - BOSS_HOLE_DEPTH)))
    if slotted:
        # flat cut facing the neighbouring boss, stopping at a ledge
        fl = (cq.Workplane("XY").box(2 * SBOSS_RB + 8, SBOSS_RB + 6, BOSS_H, centered=(True, False, False))
              .translate((x, y + FLAT_OFF, T + FLAT_Z)))
        # radial U-slot with a V bottom through the wall on the flat side
        w = SLOT_W / 2
        sl = (cq.Workplane("XZ")
              .polyline([(-w, top + 1), (w, top + 1), (w, top - SLOT_DEPTH),
                         (0, top - SLOT_DEPTH - w), (-w, top - SLOT_DEPTH)]).close()
              .extrude(-(SBOSS_RB + 3))
              .translate((x, y, 0)))
        cut = fl.union(sl)
        if flat_dir < 0:
            cut = cut.mirror("XZ", (x, y, 0))
        b = b.cut(cut)
    return b


def link1():
    pads = (cq.Workplane("XY").pushPoints([(-L1_X, L1_Y), (L1_X, L1_Y)])
            .circle(L1_PAD_R).extrude(T_LINK))
    # pads are flattened on the -Y side
    keep = (cq.Workplane("XY").box(2 * L1_X + 4 * L1_PAD_R, 4 * L1_PAD_R, T_LINK + 2, centered=False)
            .translate((-L1_X - 2 * L1_PAD_R, L1_Y - L1_FLAT, -1)))
    pads = pads.intersect(keep)
    bar = (cq.Workplane("XY").moveTo(-L1_X, L1_Y).lineTo(L1_X, L1_Y)
           .lineTo(L1_X, L1_Y + L1_BAR_END)
           .threePointArc((0, L1_Y + L1_BAR_MID), (-L1_X, L1_Y + L1_BAR_END)).close()
           .extrude(T_LINK))
    lk = pads.union(bar)
    try:
        lk = (lk.edges("|Z").edges(cq.selectors.BoxSelector((-L1_X + 1, L1_Y - 1, -1),
                                                             (L1_X - 1, L1_Y + 8, T_LINK + 1)))
              .fillet(L1_BLEND))
    except Exception:
        pass
    lk = lk.cut(cq.Workplane("XY").pushPoints([(-L1_X, L1_Y), (L1_X, L1_Y)])
                .circle(L_HOLE_D / 2).extrude(T_LINK + 2).translate((0, 0, -1)))
    try:
        lk = lk.faces(">Z").edges().fillet(LINK_FILLET)
    except Exception:
        pass
    return lk


def arm_outline(h):
    return (cq.Workplane("XY").moveTo(L2_X1 - 1.5, L2_ARM_TOP).lineTo(L2_END_X, L2_ARM_TOP)
            .lineTo(*L2_ARM_TAN)
            .threePointArc(L2_ARM_MID, (L2_X1 - 1.5, L2_ARM_BOT)).close().extrude(h))


def link2():
    frame = (cq.Workplane("XY").box(L2_X1 - L2_X0, L2_Y1 - L2_Y0, L2_LOW, centered=False)
             .edges("|Z").fillet(1.0)
             .translate((L2_X0, L2_Y0, 0)))
    low = frame.union(arm_outline(L2_LOW))
    # concave corners where the arm meets the frame
    try:
        low = (low.edges("|Z").edges(cq.selectors.BoxSelector((L2_X1 - 0.5, 69.0, -1),
                                                               (L2_X1 + 0.5, 81.0, T_LINK + 1)))
               .fillet(1.2))
    except Exception:
        pass
    # stadium opening
    opening = (cq.Workplane("XY").center(*L2_SLOT_C)
               .slot2D(L2_SLOT_L + 2 * L2_SLOT_R, 2 * L2_SLOT_R).extrude(T_LINK + 2)
               .translate((0, 0, -1)))
    low = low.cut(opening)
    try:
        low = low.faces(">Z").edges().fillet(0.4)
    except Exception:
        pass
    # square boss
    sq = (cq.Workplane("XY").box(L2_SQ, L2_SQ_Y, T_LINK, centered=False)
          .edges("|Z").fillet(0.8)
          .translate((L2_X0, L2_Y0, 0)))
    try:
        sq = sq.faces(">Z").edges().fillet(LINK_FILLET)
    except Exception:
        pass
    # round end pad with a conical ramp up from the arm
    end = (cq.Workplane("XY").center(L2_END_X, L2_HOLE_Y).circle(L2_END_R).extrude(T_LINK)
           .rotate((L2_END_X, L2_HOLE_Y, 0), (L2_END_X, L2_HOLE_Y, 1), 90))
    try:
        end = end.faces(">Z").edges().fillet(LINK_FILLET)
    except Exception:
        pass
    ramp_c = cq.Solid.makeCone(L2_END_R + 1.9, L2_END_R - LINK_FILLET, T_LINK - L2_LOW,
                               cq.Vector(L2_END_X, L2_HOLE_Y, L2_LOW), cq.Vector(0, 0, 1))
    ramp = cq.Workplane("XY").add(ramp_c).intersect(arm_outline(T_LINK))
    lk = low.union(sq).union(end).union(ramp)
    lk = lk.cut(cq.Workplane("XY").pushPoints([(L2_SQ_HOLE_X, L2_HOLE_Y), (L2_END_X, L2_HOLE_Y)])
                .circle(L_HOLE_D / 2).extrude(T_LINK + 2).translate((0, 0, -1)))
    return lk


part = ring_body()
for by in BOSS_Y:
    part = part.union(boss(BOSS_X, by, False, 0))
part = part.union(boss(-BOSS_X, BOSS_Y[0], True, -1))
part = part.union(boss(-BOSS_X, BOSS_Y[1], True, +1))

result = part.union(link1()).union(link2())

VIEW = {"azimuth": 45, "elevation": 26}
